import cadquery as cq
import math

# =====================================================================
# Close-coupler style part: body A = coupler pocket on an inclined arm
# with a keyhole pivot eye; body B = separate post (pin) with base plate.
# Units: mm.  X: across the pocket, Y: along the arm (+Y to the eye),
# Z: up (eye underside at Z = 0).
# =====================================================================

# ---------------- pocket block ----------------
BW = 18.0          # block width (X)
BD = 11.75         # block depth (Y)
BH = 11.1          # block height (Z)
BZ0 = 10.4         # block underside height
WALL = 1.0         # side / top / bottom wall
FWALL = 1.0        # front (-Y) wall
RIM = 0.45         # mouth rim step inset
RIM_D = 0.8        # mouth rim step depth

# front window (only on -X side)
WIN_X0, WIN_X1 = -9.0, -3.85
WIN_Z0, WIN_Z1 = 14.2, 17.6

# latch tabs on both sides
TAB_GAP = 0.85     # gap between block and tab
TAB_T = 1.87       # tab thickness (X)
TAB_Y0, TAB_Y1 = 1.57, 16.5
TAB_Z0, TAB_Z1 = 12.8, 18.9
HOOK = 1.2         # hook lip protrusion inward
HOOK_Y0, HOOK_Y1 = 13.4, 14.05
BRIDGE_Y0, BRIDGE_Y1 = 4.5, 5.3
BRIDGE_Z0, BRIDGE_Z1 = 14.2, 17.6

# ---------------- arm ----------------
AX = 0.3           # small lateral offset of arm / eye
AW = 11.9          # arm width (X)
SLOT_W = 6.8       # slot between rails
SLOT_FR = 0.5      # slot end corner radius
ARM_TOP_KNEE = 8.8 # where the arm top leaves the block underside
ARM_FLAT_Z = 6.7   # top of arm near the head
ARM_FLAT_Y = 17.7
XBAR_Y0 = 22.5     # cross bar
BOT_KNEE_Y, BOT_KNEE_Z = 21.0, 2.0   # arm underside knee
BOT_END_Y = 24.0   # arm underside meets the eye underside
HEAD_Y0 = 24.15    # start of head
XHOLE_R = 0.95
XHOLE_Z = 3.2

# ---------------- head / eye ----------------
NECK_W = 11.26     # cross bar / neck width (slightly narrower than rails)
EYE_YC = 30.6      # eye centre
EYE_R = 6.14       # outer radius of the eye
EYE_HOLE_R = 3.7
EYE_T = 3.1        # eye thickness
KEY_W = 3.7        # keyhole slot width
KEY_FLARE_Y0, KEY_FLARE_Y1, KEY_FLARE_W = 27.6, 29.0, 6.7
HEAD_Y0R = 24.15   # start of raised head
HEAD_TOP = 7.9     # peak of raised head
HEAD_MID_Y, HEAD_MID_Z = 29.5, 5.96
HEAD_END_Y, HEAD_END_Z = 30.8, 3.1

# ---------------- post (separate body) ----------------
PX = 33.0          # post centre X
PW = 5.0           # post width (X)
PY0, PY1 = 15.47, 17.9
PZ0, PZ1 = 3.5, 32.3
PHOLE_R = 0.75
PH_TOP_Z = PZ1 - PW / 2.0
PH_BOT_Z = 7.5
CSK_R = 2.45       # upper countersink
CSK_D = 1.3
CSK2_R = 1.3       # lower countersink
CSK2_D = 0.55
CH_R = 0.85        # channel radius
LEG_R = 0.5        # lower diverging channels
VG_W = 4.7         # V groove width at face (top)
VG_D = 0.75        # V groove depth (top)
VG_W_BOT = 2.4     # V groove width at the lower hole
VG_D_BOT = 0.6     # V groove depth at the lower hole
PLATE_Y1 = 23.5
PLATE_Z0 = 3.85     # plate underside (post foot sticks out below)
PLATE_T = 0.9
BOSS_YC = 20.4
BOSS_R = 2.05
BOSS_Z0 = 1.5
CB_R = 1.48
CB_D = 0.45
THR_R = 0.53
BORE_R = 1.45      # bore of the snap pin (from below)
BORE_TOP = 3.5
RIB_W = 0.35       # web across the bore
NOTCH_R = 0.3


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def yz_prism(pts, x0, x1):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .polyline(pts).close().extrude(x1 - x0))


def xy_prism(pts, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, z0))
            .polyline(pts).close().extrude(z1 - z0))


def zcyl(x, y, r, z0, z1):
    return (cq.Workplane("XY", origin=(x, y, z0)).circle(r).extrude(z1 - z0))


def ycyl(x, z, r, y0, y1):
    s = cq.Solid.makeCylinder(r, y1 - y0, cq.Vector(x, y0, z), cq.Vector(0, 1, 0))
    return cq.Workplane("XY").add(s)


# =====================================================================
# Body A : pocket block
# =====================================================================
block = box(-BW / 2, BW / 2, 0, BD, BZ0, BZ0 + BH)
block = block.cut(box(-BW / 2 + WALL, BW / 2 - WALL, FWALL, BD + 1,
                      BZ0 + WALL, BZ0 + BH - WALL))
block = block.cut(box(-BW / 2 + RIM, BW / 2 - RIM, BD - RIM_D, BD + 1,
                      BZ0 + RIM, BZ0 + BH - RIM))
# window in the front wall
block = block.cut(box(WIN_X0 - 0.1, WIN_X1, -1, FWALL, WIN_Z0, WIN_Z1))

# latch tabs with hooks (rounded hook nose at the +Y end)
for s in (-1, 1):
    xi = BW / 2 + TAB_GAP            # inner face
    xo = xi + TAB_T                  # outer face
    xt = xi - HOOK                   # hook tip
    tab = (cq.Workplane("XY", origin=(0, 0, TAB_Z0))
           .moveTo(s * xo, TAB_Y0)
           .lineTo(s * xi, TAB_Y0)
           .lineTo(s * xi, HOOK_Y0)
           .lineTo(s * xt, HOOK_Y0 + 0.1)
           .lineTo(s * xt, HOOK_Y1)
           .lineTo(s * xi, HOOK_Y1 + 0.85)
           .threePointArc((s * (xi + 0.3), TAB_Y1 - 0.45), (s * (xi + 1.0), TAB_Y1))
           .lineTo(s * (xo - 0.4), TAB_Y1)
           .threePointArc((s * (xo - 0.117), TAB_Y1 - 0.117), (s * xo, TAB_Y1 - 0.4))
           .close()
           .extrude(TAB_Z1 - TAB_Z0))
    bx0, bx1 = sorted((s * (BW / 2 - 0.1), s * (xi + 0.05)))
    bridge = box(bx0, bx1, BRIDGE_Y0, BRIDGE_Y1, BRIDGE_Z0, BRIDGE_Z1)
    block = block.union(tab).union(bridge)

# =====================================================================
# Body A : inclined arm (two rails + cross bar)
# =====================================================================
def arm_bottom_z(y):
    """underside of the arm: straight incline, then a steeper run-out
    to the eye underside"""
    if y <= BOT_KNEE_Y:
        return BZ0 + (BOT_KNEE_Z - BZ0) * y / BOT_KNEE_Y
    return BOT_KNEE_Z * (BOT_END_Y - y) / (BOT_END_Y - BOT_KNEE_Y)


RAIL_END = XBAR_Y0 + 0.3
arm_pts = [(0.0, BZ0), (ARM_TOP_KNEE, BZ0), (ARM_FLAT_Y, ARM_FLAT_Z),
           (RAIL_END, ARM_FLAT_Z), (RAIL_END, arm_bottom_z(RAIL_END)),
           (BOT_KNEE_Y, BOT_KNEE_Z)]
arm = yz_prism(arm_pts, AX - AW / 2, AX + AW / 2)
slot_tool = (box(AX - SLOT_W / 2, AX + SLOT_W / 2, -1, XBAR_Y0, -1, BZ0 + 0.001)
             .edges("|Z").edges(">Y").fillet(SLOT_FR))
arm = arm.cut(slot_tool)

# =====================================================================
# Body A : head with keyhole eye
# =====================================================================
def head_outline(z0, z1):
    base = box(AX - NECK_W / 2, AX + NECK_W / 2, XBAR_Y0, EYE_YC, z0, z1)
    return base.union(zcyl(AX, EYE_YC, EYE_R, z0, z1))


head = zcyl(AX, EYE_YC, EYE_R, 0, EYE_T)
raised = head_outline(0, HEAD_TOP + 0.5).intersect(
    yz_prism([(XBAR_Y0 - 0.5, arm_bottom_z(XBAR_Y0 - 0.5)),
              (XBAR_Y0 - 0.5, ARM_FLAT_Z), (HEAD_Y0R, ARM_FLAT_Z),
              (HEAD_Y0R, HEAD_TOP), (HEAD_MID_Y, HEAD_MID_Z),
              (HEAD_END_Y, HEAD_END_Z), (HEAD_END_Y + 0.3, 0),
              (BOT_END_Y, 0), (BOT_KNEE_Y, BOT_KNEE_Z)],
             AX - EYE_R - 1, AX + EYE_R + 1))
head = head.union(raised)

bodyA = block.union(arm).union(head)
# keyhole
bodyA = bodyA.cut(zcyl(AX, EYE_YC, EYE_HOLE_R, -1, 20))
bodyA = bodyA.cut(box(AX - KEY_W / 2, AX + KEY_W / 2, HEAD_Y0R, EYE_YC, -1, 20))
# flared entry of the keyhole slot into the eye
bodyA = bodyA.cut(xy_prism([(AX - KEY_W / 2, KEY_FLARE_Y0), (AX + KEY_W / 2, KEY_FLARE_Y0),
                            (AX + KEY_FLARE_W / 2, KEY_FLARE_Y1),
                            (AX - KEY_FLARE_W / 2, KEY_FLARE_Y1)], -1, 20))
# small hole through the cross bar into the keyhole slot
bodyA = bodyA.cut(ycyl(AX, XHOLE_Z, XHOLE_R, XBAR_Y0 - 1, HEAD_Y0R + 0.5))

# =====================================================================
# Body B : post with base plate and boss
# =====================================================================
post = box(PX - PW / 2, PX + PW / 2, PY0, PY1, PZ0, PZ1 - PW / 2)
post = post.union(ycyl(PX, PZ1 - PW / 2, PW / 2, PY0, PY1))

# wire groove on both broad faces (identical front and back): shallow V +
# round channel between two countersunk holes, and two channels running
# from the lower hole to the bottom corners
for fy, sy in ((PY0, 1), (PY1, -1)):
    def vtri(z, w, d):
        return cq.Wire.makePolygon([cq.Vector(PX - w / 2, fy - sy * 0.01, z),
                                    cq.Vector(PX + w / 2, fy - sy * 0.01, z),
                                    cq.Vector(PX, fy + sy * d, z)], close=True)
    # tapered V: full width at the upper hole, narrow at the lower hole
    vgroove = cq.Solid.makeLoft([vtri(PH_BOT_Z, VG_W_BOT, VG_D_BOT),
                                 vtri(PH_TOP_Z, VG_W, VG_D)], True)
    post = post.cut(cq.Workplane("XY").add(vgroove))
    post = post.cut(zcyl(PX, fy, CH_R, PH_BOT_Z, PH_TOP_Z))
    for zc, rc, dc in ((PH_TOP_Z, CSK_R, CSK_D), (PH_BOT_Z, CSK2_R, CSK2_D)):
        cone = cq.Solid.makeCone(rc, PHOLE_R, dc, cq.Vector(PX, fy - sy * 0.001, zc),
                                 cq.Vector(0, sy, 0))
        post = post.cut(cq.Workplane("XY").add(cone))
    for xs in (-1, 1):
        p0 = cq.Vector(PX, fy - sy * 0.05, PH_BOT_Z)
        p1 = cq.Vector(PX + xs * (PW / 2 + 0.3), fy - sy * 0.05, PZ0 - 0.3)
        d = p1 - p0
        leg = cq.Solid.makeCylinder(LEG_R, d.Length, p0, d.normalized())
        post = post.cut(cq.Workplane("XY").add(leg))
for zc in (PH_TOP_Z, PH_BOT_Z):
    post = post.cut(ycyl(PX, zc, PHOLE_R, PY0 - 1, PY1 + 1))

# base plate
plate = box(PX - PW / 2, PX + PW / 2, PY0, PLATE_Y1, PLATE_Z0, PLATE_Z0 + PLATE_T)
for yc in (PY1 + 0.4, PLATE_Y1 - 0.85):
    for xs in (-1, 1):
        plate = plate.cut(zcyl(PX + xs * PW / 2, yc, NOTCH_R, PZ0 - 1, PLATE_Z0 + PLATE_T + 1))
plate = plate.cut(xy_prism([(PX - 0.53, PLATE_Y1 + 0.01), (PX + 0.53, PLATE_Y1 + 0.01),
                            (PX, PLATE_Y1 - 0.42)], PZ0 - 1, PLATE_Z0 + PLATE_T + 1))
post = post.union(plate)
post = post.union(zcyl(PX, BOSS_YC, BOSS_R, BOSS_Z0, PLATE_Z0 + 0.01))
post = post.cut(zcyl(PX, BOSS_YC, CB_R, PLATE_Z0 + PLATE_T - CB_D, PLATE_Z0 + PLATE_T + 1))
post = post.cut(zcyl(PX, BOSS_YC, THR_R, BOSS_Z0 - 1, PLATE_Z0 + PLATE_T + 1))
# the boss is hollow from below, with a thin web across the bore
rib = (cq.Workplane("XY", origin=(PX, BOSS_YC, BOSS_Z0 - 1))
       .transformed(rotate=(0, 0, -45))
       .rect(2 * BORE_R + 1, RIB_W).extrude(BORE_TOP - BOSS_Z0 + 2))
post = post.cut(zcyl(PX, BOSS_YC, BORE_R, BOSS_Z0 - 1, BORE_TOP).cut(rib))

result = bodyA.union(post)

VIEW = {"azimuth": 45, "elevation": 26}
